import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
OUTER_D      = 60.0    # flange outer diameter
FLANGE_T1    = 2.35    # front flange rim thickness (hub side)
FLANGE_T2    = 2.35    # back flange rim thickness (cone side)
GROOVE_W     = 16.1    # groove width between flanges
GROOVE_DEPTH = 4.6     # depth of the round groove below the rim
HUB_D        = 26.5    # front hub diameter
HUB_L        = 10.3    # hub protrusion length
HUB_FILLET   = 5.3     # round on the hub front edge
CONE_H       = 4.7     # axial height of the conical back face
CONE_TOP_D   = 27.2    # flat diameter at the top of the back cone
BORE_D       = 12.0    # D-bore diameter (from the back)
BORE_FLAT    = 4.0     # distance from axis to the D flat
BORE_DEPTH   = 20.0    # blind bore depth
SEAM_ANGLE   = 130.0   # rotation of the revolve seam about the axis (cosmetic)

R = OUTER_D / 2.0
hub_r = HUB_D / 2.0
y_groove0 = FLANGE_T1
y_groove1 = FLANGE_T1 + GROOVE_W
y_back_rim = y_groove1 + FLANGE_T2
y_back = y_back_rim + CONE_H

# ---------------- revolved body (axis = Y, hub toward -Y) -------------
# profile drawn in the XY plane: x = radius, y = axial position
f = HUB_FILLET
c45 = math.cos(math.radians(45))
prof = (
    cq.Workplane("XY")
    .moveTo(0, -HUB_L)
    .lineTo(hub_r - f, -HUB_L)
    .threePointArc((hub_r - f + f * c45, -HUB_L + f - f * c45), (hub_r, -HUB_L + f))
    .lineTo(hub_r, 0)
    .lineTo(R, 0)
    .lineTo(R, y_groove0)
    .threePointArc((R - GROOVE_DEPTH, (y_groove0 + y_groove1) / 2.0), (R, y_groove1))
    .lineTo(R, y_back_rim)
    .lineTo(CONE_TOP_D / 2.0, y_back)
    .lineTo(0, y_back)
    .close()
)
body = prof.revolve(360, (0, 0, 0), (0, 1, 0))
# turn the revolve seam toward the lower-back side where it is least visible
body = body.rotate((0, 0, 0), (0, 1, 0), SEAM_ANGLE)

# ---------------- D-shaped blind bore from the back face -------------
r_b = BORE_D / 2.0
h_b = math.sqrt(r_b ** 2 - BORE_FLAT ** 2)
# XZ workplane: local x = +X, local y = +Z, normal = -Y (into the part)
bore = (
    cq.Workplane("XZ", origin=(0, y_back, 0))
    .moveTo(-BORE_FLAT, -h_b)
    .lineTo(-BORE_FLAT, h_b)
    .threePointArc((r_b, 0), (-BORE_FLAT, -h_b))
    .close()
    .extrude(BORE_DEPTH)
)

result = body.cut(bore)

VIEW = {"azimuth": 45, "elevation": 26}
